import math
import cadquery as cq

# ============================================================ parameters (mm)
# oval body: lower part of a spheroid (revolved about a Y-parallel axis) with
# a rounded rim ring on top and a recessed top panel
BODY_HALF_W = 36.0      # half width of the top oval (X)
BODY_HALF_L = 84.25     # half length of the top oval (Y)
BODY_CY = 1.75          # oval centre is shifted a little towards the tail (+Y)
BODY_DEPTH = 48.6       # rim crest to the lowest point of the bowl
RIM_H = 7.0             # rim ring height above the panel
RIM_TOP = 1.0           # height of the rim crest above the reference plane z=0
RIM_SCALE = 0.81        # inner oval of the rim = RIM_SCALE * outer oval
RIM_FILLET_OUT = 3.2
RIM_FILLET_IN = 3.5
BAND_BOT = -15.0        # lower edge of the proud band (tick line)
BAND_PROUD = 0.6

EYE_R = 4.6
EYE_X = 14.0
EYE_Z = -12.8
EYE_PROUD = 3.0
EYE_TILT = 15.0        # outward tilt of the eye axis from -Y (deg)

PIVOT_R = 8.0                       # wing pivot ball
PIVOT_C = (-44.6, 7.5, -15.0)       # left ball centre (right side mirrored)
WING_O = (-43.9, 7.0, -15.4)        # wing plane origin (pivot point)
GEAR_R = 4.6                        # gear on the front of the ball
GEAR_T = 4.0
GEAR_TEETH = 12
SHAFT_R = 2.3
SHAFT_L = 8.0

WING_T = 1.5
WING_XDIR = (-0.7162, 0.3211, 0.6196)   # wing axis (pivot -> tip), left wing
WING_NORMAL = (-0.6384, -0.6601, -0.3958)
# leaf outline in the wing plane (u along axis from pivot, v across)
WING_OUTLINE = [
    (118.5, 0.0), (112.0, 4.2), (104.0, 7.6), (91.8, 12.3), (75.7, 16.6),
    (62.0, 18.4), (49.1, 18.5), (38.6, 16.2), (28.7, 10.9), (20.5, 4.7),
    (15.0, -0.6), (10.5, -3.2), (5.2, -4.2), (3.2, -7.1), (3.2, -10.8),
    (5.6, -13.6), (12.4, -16.4), (23.1, -18.5), (37.7, -19.5), (53.2, -19.7),
    (70.6, -18.2), (86.3, -15.8), (99.5, -12.2), (110.2, -7.4),
]
# raised veins on the inner/upper face of the wing (polylines in u, v)
VEIN_W = 0.9
VEIN_H = 0.5
WING_VEINS = [
    [(8.0, -12.5), (23.0, -16.6), (40.0, -17.8), (55.3, -17.4), (75.6, -14.6),
     (94.4, -10.0), (108.0, -4.8), (115.0, -0.8)],                    # costa
    [(12.0, -10.5), (25.0, -13.6), (42.9, -13.8), (53.5, -12.3), (65.3, -9.9),
     (75.9, -7.8), (87.7, -5.4), (101.5, -1.8), (112.0, 0.8)],        # radius
    [(75.5, -7.4), (83.3, -2.4), (92.4, 3.8), (99.5, 8.0)],
    [(75.5, -7.4), (75.6, -4.2), (72.4, -1.6), (70.0, 3.2), (66.2, 5.9),
     (64.1, 10.2), (60.4, 13.1), (59.3, 16.5)],                       # cross chain
    [(13.0, -7.5), (25.0, -9.6), (38.6, -9.8), (57.8, -5.2), (72.4, -1.6)],
    [(14.0, -4.0), (27.0, -3.0), (39.7, -0.9), (52.3, 2.4), (66.2, 5.9)],
    [(16.0, 0.0), (30.0, 5.0), (44.0, 10.0), (57.0, 14.0)],
    [(91.6, 4.6), (89.7, 8.4), (87.8, 11.3)],
    [(87.8, 11.3), (79.5, 5.1), (72.5, -0.8)],
    [(81.4, 12.3), (76.3, 6.8), (70.0, 3.2)],
    [(75.4, 14.2), (66.2, 5.9)],
    [(69.4, 15.6), (64.1, 10.2)],
    [(64.6, 16.8), (60.4, 13.1)],
]

LEG_Y = (-30.0, 46.0)   # front / rear leg stations
LEG_T = 4.4             # arm thickness (Y)
BRACKET = (10.0, 8.5)   # bracket length in Y, height
BRACKET_TILT = -15.0    # outer end of the bracket dips (deg about Y)
WHEEL_R = 5.0
WHEEL_T = 4.6
WHEEL_X = -62.0
WHEEL_Z = -52.5

REARBOX = (-37.0, -18.0, 34.0, 60.0, -35.0, -8.0)  # x0,x1,y0,y1,z0,z1
TAIL_X = -25.0
POST_T = 6.0
JAW_T = 3.0
KNOB_Z = -20.0
KNOB_R = 10.5
KNOB_Y0 = 62.0          # tail cylinder starts inside the body here

# ============================================================ body
panel_z = RIM_TOP - RIM_H
depth = BODY_DEPTH - RIM_H
# circle section (radius R, centre h below the panel) that is BODY_HALF_W wide
# at the panel plane and `depth` deep below it
R_sec = 0.5 * (depth + BODY_HALF_W ** 2 / depth)
h_sec = depth - R_sec                     # centre offset below panel plane
L_sec = BODY_HALF_L / math.sqrt(1.0 - (h_sec / R_sec) ** 2)
axis_z = panel_z - h_sec

spheroid = (cq.Workplane("YZ", origin=(0, BODY_CY, axis_z))
            .ellipseArc(L_sec, R_sec, 0, 180, startAtCurrent=False).close()
            .revolve(360, (0, 0, 0), (1, 0, 0)))
cutter = cq.Workplane("XY").box(400, 400, 200).translate((0, 0, panel_z + 100))
bowl = spheroid.cut(cutter)

rim = (cq.Workplane("XY", origin=(0, BODY_CY, panel_z))
       .ellipse(BODY_HALF_W, BODY_HALF_L).extrude(RIM_H)
       .cut(cq.Workplane("XY", origin=(0, BODY_CY, panel_z))
            .ellipse(BODY_HALF_W * RIM_SCALE, BODY_HALF_L * RIM_SCALE)
            .extrude(RIM_H)))
top_edges = rim.faces(">Z").edges().vals()
outer_e = max(top_edges, key=lambda e: e.BoundingBox().xlen)
inner_e = min(top_edges, key=lambda e: e.BoundingBox().xlen)
rim_solid = rim.val().fillet(RIM_FILLET_OUT, [outer_e])
top_edges = [e for e in rim_solid.Edges()
             if abs(e.BoundingBox().zmax - RIM_TOP) < 1e-6
             and abs(e.BoundingBox().zmin - RIM_TOP) < 1e-6]
inner_e = min(top_edges, key=lambda e: e.BoundingBox().xlen)
rim_solid = rim_solid.fillet(RIM_FILLET_IN, [inner_e])
rim = cq.Workplane("XY").add(rim_solid)
# slightly proud band between the rim and the tick line
band = (cq.Workplane("YZ", origin=(0, BODY_CY, axis_z))
        .ellipseArc(L_sec + BAND_PROUD, R_sec + BAND_PROUD, 0, 180,
                    startAtCurrent=False).close()
        .revolve(360, (0, 0, 0), (1, 0, 0)))
band = band.intersect(cq.Workplane("XY").box(400, 400, panel_z - BAND_BOT, centered=(True, True, False))
                      .translate((0, 0, BAND_BOT)))
body = bowl.union(band).union(rim)


def body_y(x, z):
    """+Y extent of the bowl surface at (x, z)."""
    r2 = x * x + (z - axis_z) ** 2
    v = 1.0 - r2 / R_sec ** 2
    return L_sec * math.sqrt(max(v, 0.0))


# ============================================================ left side parts
side = cq.Workplane("XY")

# eye disc on the front end
ey = body_y(EYE_X, EYE_Z) - BODY_CY      # front surface is at y = -ey
et = math.radians(EYE_TILT)
eye_dir = (-math.sin(et), -math.cos(et), 0.0)
eye_plane = cq.Plane(origin=(-EYE_X, -ey, EYE_Z), xDir=(math.cos(et), -math.sin(et), 0),
                     normal=eye_dir)
eye = (cq.Workplane(eye_plane).workplane(offset=-6.0).circle(EYE_R)
       .extrude(6.0 + EYE_PROUD))
side = side.union(eye)

# wing pivot ball with stub to the body
px, py, pz = PIVOT_C
ball = cq.Workplane("XY").sphere(PIVOT_R).translate(PIVOT_C)
stub = (cq.Workplane("YZ", origin=(-28.0, 0, 0)).center(py, pz)
        .circle(4.5).extrude(-(abs(px) - 28.0)))
side = side.union(ball).union(stub)

# gear + shaft on the front of the ball (axis Y)
gx, gz = px - 1.5, pz + 1.3
g_y0 = py - 9.5
gear = (cq.Workplane("XZ", origin=(0, g_y0 + GEAR_T, 0)).center(gx, gz)
        .circle(GEAR_R - 0.6).extrude(GEAR_T))
for i in range(GEAR_TEETH):
    ang = 360.0 / GEAR_TEETH * i
    tooth = (cq.Workplane("XZ", origin=(0, g_y0 + GEAR_T, 0)).center(gx, gz)
             .transformed(rotate=(0, 0, ang))
             .center(GEAR_R - 0.4, 0).rect(1.6, 1.3).extrude(GEAR_T))
    gear = gear.union(tooth)
shaft = (cq.Workplane("XZ", origin=(0, g_y0 + 0.5, 0)).center(gx, gz)
         .circle(SHAFT_R).extrude(SHAFT_L))
side = side.union(gear).union(shaft)

# wing: flat leaf plate in its own plane through the ball centre
wing_plane = cq.Plane(origin=WING_O, xDir=WING_XDIR, normal=WING_NORMAL)
# outline as a chain of circular arcs through consecutive outline points
wing_wp = cq.Workplane(wing_plane).moveTo(*WING_OUTLINE[0])
n_out = len(WING_OUTLINE)
for i in range(0, n_out, 2):
    wing_wp = wing_wp.threePointArc(WING_OUTLINE[(i + 1) % n_out],
                                    WING_OUTLINE[(i + 2) % n_out])
wing = wing_wp.close().extrude(WING_T / 2, both=True)
vein_wp = cq.Workplane(wing_plane).workplane(offset=-WING_T / 2)
veins = []
for pts in WING_VEINS:
    for (u0, v0), (u1, v1) in zip(pts[:-1], pts[1:]):
        seg = math.hypot(u1 - u0, v1 - v0)
        ang = math.degrees(math.atan2(v1 - v0, u1 - u0))
        veins.append(vein_wp.moveTo((u0 + u1) / 2, (v0 + v1) / 2)
                     .slot2D(seg + VEIN_W, VEIN_W, ang)
                     .extrude(-VEIN_H).val())
wing = cq.Workplane("XY").add(wing.val().fuse(*veins).clean())
side = side.union(wing)


# legs: tilted bracket, curved arm, wheel
def make_leg(yc, x_in):
    bl, bh = BRACKET
    bx0, bx1 = -51.5, -x_in
    br = (cq.Workplane("XY").box(bx1 - bx0, bl, bh)
          .translate(((bx0 + bx1) / 2, yc, -25.0))
          .rotate((-44.0, yc, -25.0), (-44.0, yc + 1, -25.0), BRACKET_TILT))
    arm = (cq.Workplane("XZ", origin=(0, yc + LEG_T / 2, 0))
           .moveTo(-52.0, -24.0)
           .threePointArc((-60.2, -29.6), (-62.3, -37.5))
           .lineTo(-63.3, WHEEL_Z + 2.0)
           .lineTo(-58.9, WHEEL_Z + 2.0)
           .lineTo(-58.2, -43.0)
           .threePointArc((-56.2, -36.3), (-50.5, -31.0))
           .close()
           .extrude(LEG_T))
    wheel = (cq.Workplane("YZ", origin=(WHEEL_X - WHEEL_T / 2, 0, 0))
             .center(yc, WHEEL_Z).circle(WHEEL_R).extrude(WHEEL_T))
    return br.union(arm).union(wheel)


for yl, xin in zip(LEG_Y, (27.0, 30.0)):
    side = side.union(make_leg(yl, xin))

# rear side box
x0, x1, y0, y1, z0, z1 = REARBOX
rbox = (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False)
        .translate((x0, y0, z0)))
side = side.union(rbox)
# small joint ball on the rear box face above the rear leg
side = side.union(cq.Workplane("XY").sphere(3.6).translate((x0, LEG_Y[1] - 1.5, -15.0)))

# tail post + two jaws (profiles in the YZ plane)
post = (cq.Workplane("YZ", origin=(TAIL_X - POST_T / 2, 0, 0))
        .moveTo(57.0, -34.8)
        .lineTo(57.0, -14.0)
        .threePointArc((66.0, -4.0), (69.8, 18.3))
        .lineTo(74.2, 18.3)
        .threePointArc((78.5, 0.0), (81.0, -34.8))
        .close()
        .extrude(POST_T))
jaw_up = (cq.Workplane("YZ", origin=(TAIL_X - JAW_T / 2, 0, 0))
          .polyline([(73.0, 18.3), (78.8, 18.3), (97.9, 3.9), (80.2, -3.5),
                     (76.0, -3.5)]).close().extrude(JAW_T))
jaw_lo = (cq.Workplane("YZ", origin=(TAIL_X - JAW_T / 2, 0, 0))
          .polyline([(78.0, -7.5), (98.9, -7.5), (86.1, -33.8), (78.0, -33.8)])
          .close().extrude(JAW_T))
side = side.union(post).union(jaw_up).union(jaw_lo)

# ============================================================ assemble
result = body.union(side).union(side.mirror("YZ"))

# rear knob (stepped cylinder on the tail end)
y_end = BODY_CY + BODY_HALF_L
knob = (cq.Workplane("XZ", origin=(0, y_end + 2.5, 0)).center(0, KNOB_Z)
        .circle(KNOB_R).extrude(y_end + 2.5 - KNOB_Y0))
knob2 = (cq.Workplane("XZ", origin=(0, y_end + 4.8, 0)).center(0, KNOB_Z)
         .circle(KNOB_R - 2.0).extrude(2.3))
result = result.union(knob).union(knob2)

VIEW = {"azimuth": 45, "elevation": 26}
